import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
R_OUT = 100.0          # tube outer radius
T_TUBE = 2.0           # thin tube wall
L_TOTAL = 543.0        # overall length along X
L_FLANGE = 23.5        # end flange length
L_COLLAR = 47.0        # machined collar length (behind flange)
X_COLLAR = L_TOTAL - L_FLANGE - L_COLLAR   # collar start (joint with thin tube)
X_FLANGE = L_TOTAL - L_FLANGE              # flange start
R_FLANGE = 97.5        # flange outer radius (slightly stepped down)
R_LIP = 77.0           # smallest bore (front lip)
LIP_DEPTH = 9.0
R_COLLAR_IN = 95.0     # collar bore
X_BORE_STEP = X_COLLAR + 2.5   # thin-tube bore steps down to the collar bore
R_PCD = 82.4           # face bolt circle radius
D_FACE_HOLE = 3.5
N_FACE_HOLES = 6
FACE_HOLE_START = 44.0
CH_FACE = 0.6          # small chamfer on the flange face outer edge
SEAM_ANGLE = 310.0     # where the outer revolve seam is parked (hidden at silhouettes)
SEAM_ANGLE_IN = 130.0  # same for the bore surfaces

# screw pockets around the collar (12x, every 30 deg): a 45-deg spot face for an
# inclined screw plus a shallow-angle clearance bore that runs out on the OD
N_POCKETS = 12
POCKET_R = 6.5         # clearance bore radius (pocket half-width)
POCKET_X0 = X_COLLAR + 3.5     # where the 45-deg spot face meets the OD
POCKET_TIP_X = X_COLLAR + 28.5  # where the clearance bore runs out on the OD
NOSE_TILT = 20.0       # clearance bore axis angle from the X axis (deg)
SPOT_TILT = 45.0       # spot-face normal angle from the X axis (deg)
SCREW_D = 5.0
CSINK_D = 7.5          # 90-deg countersink on the spot face

# internal pads under the pockets
PAD_W = 16.0
PAD_IN_R = 90.5        # innermost radius at collar start
PAD_END_X = X_COLLAR + 26.5     # ramp runs out into the bore here

# radial round holes
ROUND_HOLE_D = 15.0
ROUND_HOLE_X = X_COLLAR + 30.0
ROUND_HOLE_ANGLES = (15.0, 195.0, 285.0)

# axial slits with relief holes, and plain small holes
SLIT_ANGLES = (36.0, 81.0, 171.0, 216.0, 321.0)
SMALL_HOLE_ANGLES = (126.0, 261.0, 306.0, 351.0)
SLIT_W = 0.6
SLIT_END_X = X_COLLAR + 31.5
SLIT_HOLE_D = 3.0

ORIGIN = cq.Vector(0, 0, 0)
XAXIS = cq.Vector(1, 0, 0)


def polar(solid, n, start=0.0, step=None):
    step = 360.0 / n if step is None else step
    out = None
    for k in range(n):
        s = solid.rotate(ORIGIN, XAXIS, start + step * k)
        out = s if out is None else out.fuse(s)
    return out


# ---- main body: outer envelope minus bore (separate revolves so that the
#      periodic seams of outer and inner surfaces sit where they stay hidden) ----
outer = (cq.Workplane("XY").moveTo(0, 0).lineTo(0, R_OUT).lineTo(X_COLLAR, R_OUT)
         .lineTo(X_FLANGE, R_OUT).lineTo(X_FLANGE, R_FLANGE)
         .lineTo(L_TOTAL - CH_FACE, R_FLANGE).lineTo(L_TOTAL, R_FLANGE - CH_FACE)
         .lineTo(L_TOTAL, 0).close()
         .revolve(360, (0, 0, 0), (1, 0, 0), clean=False)
         .rotate((0, 0, 0), (1, 0, 0), SEAM_ANGLE))
bore_prof = [
    (-1.0, 0), (-1.0, R_OUT - T_TUBE), (X_BORE_STEP, R_OUT - T_TUBE),
    (X_BORE_STEP, R_COLLAR_IN), (L_TOTAL - LIP_DEPTH, R_COLLAR_IN),
    (L_TOTAL - LIP_DEPTH, R_LIP), (L_TOTAL + 1.0, R_LIP), (L_TOTAL + 1.0, 0),
]
bore = (cq.Workplane("XY").polyline(bore_prof).close()
        .revolve(360, (0, 0, 0), (1, 0, 0), clean=False)
        .rotate((0, 0, 0), (1, 0, 0), SEAM_ANGLE_IN))
body = outer.cut(bore, clean=False)

# ---- internal pads (one under each pocket), arc ramp tangent to the bore ----
_L = PAD_END_X - X_BORE_STEP
_h = R_COLLAR_IN - PAD_IN_R
_rp = (_L ** 2 + _h ** 2) / (2.0 * _h)            # arc radius, tangent at PAD_END_X
pad_mid_x = (X_BORE_STEP + PAD_END_X) / 2.0
pad_mid_r = R_COLLAR_IN - _rp + math.sqrt(_rp ** 2 - (pad_mid_x - PAD_END_X) ** 2)
pad_ring = (cq.Workplane("XY")
            .moveTo(X_BORE_STEP, R_COLLAR_IN + 1.0).lineTo(X_BORE_STEP, PAD_IN_R)
            .threePointArc((pad_mid_x, pad_mid_r), (PAD_END_X, R_COLLAR_IN))
            .lineTo(PAD_END_X, R_COLLAR_IN + 1.0).close()
            .revolve(360, (0, 0, 0), (1, 0, 0))
            .rotate((0, 0, 0), (1, 0, 0), 180.0))
_a = math.asin(PAD_W / 2.0 / PAD_IN_R)
_rr = R_OUT * 1.2
sector = (cq.Workplane("YZ").workplane(offset=X_BORE_STEP - 1.0)
          .polyline([(0, 0), (_rr * math.cos(_a), -_rr * math.sin(_a)),
                     (_rr * math.cos(_a), _rr * math.sin(_a))]).close()
          .extrude(L_COLLAR))
pad0 = pad_ring.intersect(sector).val()
pads = polar(pad0, N_POCKETS)
body = body.union(cq.Workplane().add(pads), clean=False)

# ---- face bolt holes ----
pts = [(R_PCD * math.cos(math.radians(FACE_HOLE_START + 60 * k)),
        R_PCD * math.sin(math.radians(FACE_HOLE_START + 60 * k)))
       for k in range(N_FACE_HOLES)]
holes = (cq.Workplane("YZ").workplane(offset=L_TOTAL - 15)
         .pushPoints(pts).circle(D_FACE_HOLE / 2).extrude(20))
body = body.cut(holes, clean=False)

# ---- screw pockets: spot face + clearance bore + inclined screw hole ----
gn = math.radians(NOSE_TILT)
gsp = math.radians(SPOT_TILT)
dn = cq.Vector(math.cos(gn), math.sin(gn), 0)
# lowest generatrix of the clearance bore passes through (POCKET_TIP_X, R_OUT)
axis_pt = cq.Vector(POCKET_TIP_X - POCKET_R * math.sin(gn),
                    R_OUT + POCKET_R * math.cos(gn), 0)
nose = cq.Solid.makeCylinder(POCKET_R, 60.0, axis_pt - dn * 35.0, dn)
ns = (math.cos(gsp), math.sin(gsp))               # spot-face normal (X, r)
tx, tr = -ns[1], ns[0]                             # spot-face direction in X-r
half = (cq.Workplane("XY", origin=(0, 0, -20.0))
        .polyline([(POCKET_X0 - 20 * tx, R_OUT - 20 * tr),
                   (POCKET_X0 + 20 * tx, R_OUT + 20 * tr),
                   (POCKET_X0 + 60.0, R_OUT + 20 * tr),
                   (POCKET_X0 + 60.0, R_OUT - 20 * tr)]).close()
        .extrude(40.0).val())
slot = nose.intersect(half)
# deepest point of the pocket (bore floor meets spot face) and spot-face centre
_t = ((POCKET_X0 - POCKET_TIP_X) * ns[0]) / (math.cos(gn) * ns[0] + math.sin(gn) * ns[1])
deep = (POCKET_TIP_X + _t * math.cos(gn), R_OUT + _t * math.sin(gn))
spot_c = cq.Vector((POCKET_X0 + deep[0]) / 2.0, (R_OUT + deep[1]) / 2.0, 0)
sdir = cq.Vector(-ns[0], -ns[1], 0)
screw = cq.Solid.makeCylinder(SCREW_D / 2, 16.0, spot_c - sdir * 2.0, sdir)
_cs = CSINK_D / 2.0 + 0.5
csink = cq.Solid.makeCone(_cs, 0.0, _cs, spot_c - sdir * 0.5, sdir)
pocket0 = slot.fuse(screw).fuse(csink)
pockets = polar(pocket0, N_POCKETS)
body = body.cut(cq.Workplane().add(pockets), clean=False)

# ---- radial round holes ----
for ang in ROUND_HOLE_ANGLES:
    hc = cq.Solid.makeCylinder(ROUND_HOLE_D / 2, 30.0,
                               cq.Vector(ROUND_HOLE_X, 80.0, 0), cq.Vector(0, 1, 0))
    body = body.cut(cq.Workplane().add(hc.rotate(ORIGIN, XAXIS, ang)), clean=False)

# ---- axial slits ending in relief holes ----
slit_len = SLIT_END_X - X_COLLAR
sl = cq.Solid.makeBox(slit_len + 1.0, 20.0, SLIT_W,
                      cq.Vector(X_COLLAR - 1.0, R_OUT - 18.0, -SLIT_W / 2))
rh = cq.Solid.makeCylinder(SLIT_HOLE_D / 2, 20.0,
                           cq.Vector(SLIT_END_X, R_OUT - 18.0, 0), cq.Vector(0, 1, 0))
slit0 = sl.fuse(rh)
cutters = None
for ang in SLIT_ANGLES:
    c = slit0.rotate(ORIGIN, XAXIS, ang)
    cutters = c if cutters is None else cutters.fuse(c)
for ang in SMALL_HOLE_ANGLES:
    cutters = cutters.fuse(rh.rotate(ORIGIN, XAXIS, ang))
body = body.cut(cq.Workplane().add(cutters), clean=False)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
